import math
import cadquery as cq

# Cable gland (BSP 1/4") with lock nut, sealing washer, body hex,
# cap thread and domed cap nut.  Axis of the gland = global Y axis;
# lock nut at -Y (front), domed cap at +Y (back).

# ---------------- axial stations (mm) ----------------
Y_TUBE_FRONT = -0.4     # front of the entry-thread tube (protrudes from lock nut)
Y_NUT0 = 0.0            # lock-nut front face
Y_NUT1 = 5.32           # lock-nut hex end / collar start
Y_COL1 = 6.5            # lock-nut collar end
Y_WA0 = 7.51            # sealing washer front
Y_WA1 = 9.64            # washer back / body hex front
Y_BH1 = 14.61           # body hex back / cap thread start
Y_TH1 = 20.15           # cap thread end / dome-nut front
Y_DN_CH = 27.26         # start of dome-nut back chamfer (at the hex corners)
Y_DOME1 = 34.5          # dome tip

# ---------------- radial sizes (mm) ----------------
R_COLLAR = 11.65        # lock nut collar radius (= turned corner radius)
NUT_AF = 21.4           # lock nut across flats
R_WASHER = 10.57        # sealing washer
BODY_AF = 17.3          # body hex across flats
CAP_AF = 17.5           # dome-nut hex across flats
R_THREAD = 6.86         # cap thread major radius
R_THREAD_MIN = 6.0      # cap thread minor radius
THREAD_PITCH = 1.44
THREAD_FIRST_CREST = 15.63
R_ENTRY = 7.05          # entry thread major radius (inside lock nut)
R_ENTRY_EDGE = 6.5      # entry thread flank radius at collar / washer faces
R_ENTRY_ROOT = 6.03     # entry thread root visible between collar and washer
R_TUBE_FRONT = 6.08     # chamfered front edge of the tube
R_CBORE = 7.2           # lock nut counterbore
CBORE_DEPTH = 1.0
R_BORE = 4.95           # main bore
R_CONE_END = 3.87       # end of the internal taper
R_HOLE = 3.58           # cable hole through the dome
R_HOLE_GROOVE = 3.88    # internal grooves (seal thread) in the cable hole
HOLE_GROOVE_PITCH = 1.3
N_HOLE_GROOVES = 3
R_DOME = 8.42           # dome base radius
DOME_FILLET = 4.8       # dome rounding radius (short cylinder + round)
Y_BORE_CONE0 = Y_TUBE_FRONT   # long, shallow internal taper starts at the tube front
Y_BORE_CONE1 = 19.35

# marking on the body hex
TEXT = 'BSP 1/4"'
TEXT_SIZE = 2.2
TEXT_DEPTH = 0.1
TEXT_Y = 11.0

SEAM_ANGLE = 135.0      # outer revolve seams placed on the hidden lower-back side
BORE_SEAM_ANGLE = -45.0 # inner (bore) seam on the upper side, hidden when looking in


def revolve_profile(pts, seam=SEAM_ANGLE):
    """Revolve a closed (radius, y) polyline about the global Y axis."""
    return (cq.Workplane("XY").polyline(pts).close()
            .revolve(360, (0, 0, 0), (0, 1, 0))
            .rotate((0, 0, 0), (0, 1, 0), seam))


def cyl(r, y0, y1):
    return revolve_profile([(0, y0), (r, y0), (r, y1), (0, y1)])


def hex_prism(af, y0, y1):
    """Hexagon prism along +Y, flats on top/bottom (+-Z), corners at +-X."""
    ac = af / math.cos(math.radians(30))
    return (cq.Workplane("XZ", origin=(0, y0, 0))
            .polygon(6, ac)
            .extrude(-(y1 - y0)))


# ---------------- lock nut: hex with turned corners + counterbore ----------------
lock_nut = hex_prism(NUT_AF, Y_NUT0, Y_NUT1).intersect(cyl(R_COLLAR, Y_NUT0, Y_NUT1))
lock_nut = lock_nut.cut(cyl(R_CBORE, Y_NUT0 - 1.0, Y_NUT0 + CBORE_DEPTH))

# ---------------- body hex ----------------
body_hex = hex_prism(BODY_AF, Y_WA1, Y_BH1)

# ---------------- dome-nut hex with 45 deg back chamfer ----------------
cap_ac = CAP_AF / math.cos(math.radians(30))
ch_len = cap_ac / 2 - R_DOME
Y_DOME0 = Y_DN_CH + ch_len          # dome starts where the chamfer cone ends
cap_env = revolve_profile([(0, Y_TH1), (cap_ac, Y_TH1), (cap_ac, Y_DN_CH),
                           (cap_ac / 2, Y_DN_CH), (R_DOME, Y_DOME0),
                           (0, Y_DOME0)])
cap_hex = hex_prism(CAP_AF, Y_TH1, Y_DOME0).intersect(cap_env)

# ---------------- revolved core ----------------
# tube end, entry thread, collar, V groove, washer, cap thread, dome
prof = [
    (0.0, Y_TUBE_FRONT),
    (R_TUBE_FRONT, Y_TUBE_FRONT),
    (R_ENTRY, Y_TUBE_FRONT + (R_ENTRY - R_TUBE_FRONT)),   # 45 deg chamfer
    (R_ENTRY, Y_NUT1),
    (R_COLLAR, Y_NUT1),
    (R_COLLAR, Y_COL1),
    (R_ENTRY_EDGE, Y_COL1),
    (R_ENTRY_ROOT, 0.5 * (Y_COL1 + Y_WA0)),
    (R_ENTRY_EDGE, Y_WA0),
    (R_WASHER, Y_WA0),
    (R_WASHER, Y_WA1),
    (R_THREAD_MIN, Y_WA1),
]
# cap thread (plain revolved V teeth)
half = THREAD_PITCH / 2.0
c = THREAD_FIRST_CREST
prof.append((R_THREAD_MIN, c - half))
while c < Y_TH1:
    prof.append((R_THREAD, c))
    prof.append((R_THREAD_MIN, c + half))
    c += THREAD_PITCH
prof.append((R_THREAD_MIN, Y_DOME0))
prof.append((R_DOME, Y_DOME0))
prof.append((R_DOME, Y_DOME1 - DOME_FILLET))

# dome: short cylinder + large round down to the flat tip face
a45 = math.radians(45)
dome_mid = (R_DOME - DOME_FILLET + DOME_FILLET * math.cos(a45),
            Y_DOME1 - DOME_FILLET + DOME_FILLET * math.sin(a45))

core = (cq.Workplane("XY").polyline(prof)
        .threePointArc(dome_mid, (R_DOME - DOME_FILLET, Y_DOME1))
        .lineTo(0.0, Y_DOME1)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 1, 0), SEAM_ANGLE))

body = core.union(lock_nut).union(body_hex).union(cap_hex)

# ---------------- inner passage ----------------
# main bore, conical reduction, cable hole with grooves out through the dome
bp = [(0.0, Y_TUBE_FRONT - 1.0), (R_BORE, Y_TUBE_FRONT - 1.0),
      (R_BORE, Y_BORE_CONE0), (R_CONE_END, Y_BORE_CONE1),
      (R_HOLE, Y_BORE_CONE1)]
g_half = HOLE_GROOVE_PITCH / 2.0
g0 = Y_DOME1 - 0.6 - (N_HOLE_GROOVES - 1) * HOLE_GROOVE_PITCH
for i in range(N_HOLE_GROOVES):
    gc = g0 + i * HOLE_GROOVE_PITCH
    bp.append((R_HOLE, gc - g_half * 0.8))
    bp.append((R_HOLE_GROOVE, gc))
    bp.append((R_HOLE, gc + g_half * 0.8))
bp += [(R_HOLE, Y_DOME1 + 1.0), (0.0, Y_DOME1 + 1.0)]
bore = revolve_profile(bp, BORE_SEAM_ANGLE)

body = body.cut(bore)

# ---------------- engraved marking on the top flat of the body hex ----------------
try:
    tplane = cq.Plane(origin=(0, TEXT_Y, BODY_AF / 2.0), xDir=(1, 0, 0), normal=(0, 0, 1))
    txt = (cq.Workplane(tplane)
           .text(TEXT, TEXT_SIZE, -TEXT_DEPTH, combine=False, halign="center", valign="center"))
    if txt.vals():
        marked = body.cut(txt)
        if marked.val().isValid():
            body = marked
except Exception:
    pass

result = body
